import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BEAM_PITCH = 802.5      # X distance between neighbouring cross beams
N_BEAMS = 3
BEAM_W = 60.0           # beam tube width (X)
BEAM_H = 60.0           # beam tube height (Z)
BEAM_R = 14.0           # outer corner radius of the tube
BEAM_WALL = 4.0         # wall thickness

CAP_T = 6.0             # end cap on the back end of each beam
CAP_EDGE_R = 2.0
CAP_RECESS_INSET = 7.0
CAP_RECESS_D = 1.5
CAP_BOSS_D = 28.0        # round button in the middle of the cap
CAP_BOSS_H = 2.5
CAP_BOSS_FILLET = 1.5

PLATE_S = 95.0         # square foot plate at the front end
PLATE_T = 6.5
PLATE_R = 4.0
PLATE_HOLE_D = 7.0
PLATE_HOLE_INSET = 9.5
NUT_D = 13.0
NUT_L = 7.0

Y_FRONT = -311.5        # front face of the foot plates
Y_BACK = 309.0          # back face of the end caps

ROD_D = 32.0            # tie rods: round bar with a flat ground on top
ROD_FLAT = 3.0          # depth of the top flat
ROD_Y = [Y_BACK - 46.0, Y_FRONT + 278.0]   # tie rod centre lines (Y)
ROD_NUT_D = 44.0        # round clamping nuts inside the outer tubes
ROD_NUT_L = 10.0
ROD_NUT_GAP = 3.0       # gap between nut face and the tube's outer wall

SLOT_L = 39.0           # access slots in the outer face of the +X beam
SLOT_H = 30.0
SLOT_R = 13.0

beam_y0 = Y_FRONT + PLATE_T
beam_len = (Y_BACK - CAP_T) - beam_y0
beam_xs = [(i - (N_BEAMS - 1) / 2.0) * BEAM_PITCH for i in range(N_BEAMS)]


def rsq(wp, w, h, r):
    """Rounded rectangle on a workplane (centred)."""
    return wp.sketch().rect(w, h).vertices().fillet(r).finalize()


def beam_tube(length):
    """Hollow rounded-square tube along +Y starting at y=0."""
    outer = rsq(cq.Workplane("XZ"), BEAM_W, BEAM_H, BEAM_R).extrude(-length)
    inner = rsq(
        cq.Workplane("XZ", origin=(0, -1.0, 0)),
        BEAM_W - 2 * BEAM_WALL, BEAM_H - 2 * BEAM_WALL, BEAM_R - BEAM_WALL,
    ).extrude(-(length + 2.0))
    return outer.cut(inner)


def end_cap():
    cap = (
        rsq(cq.Workplane("XZ", origin=(0, Y_BACK - CAP_T, 0)), BEAM_W, BEAM_H, BEAM_R)
        .extrude(-CAP_T)
        .faces(">Y").edges().fillet(CAP_EDGE_R)
    )
    rec = rsq(
        cq.Workplane("XZ", origin=(0, Y_BACK + 1.0, 0)),
        BEAM_W - 2 * CAP_RECESS_INSET, BEAM_H - 2 * CAP_RECESS_INSET,
        BEAM_R - CAP_RECESS_INSET,
    ).extrude(CAP_RECESS_D + 1.0)
    cap = cap.cut(rec)
    boss = (
        cq.Workplane("XZ", origin=(0, Y_BACK - CAP_RECESS_D - 0.5, 0))
        .circle(CAP_BOSS_D / 2)
        .extrude(-(CAP_BOSS_H + CAP_RECESS_D + 0.5))
        .faces(">Y").edges().fillet(CAP_BOSS_FILLET)
    )
    return cap.union(boss)


def foot_plate():
    p = (
        rsq(cq.Workplane("XZ", origin=(0, Y_FRONT, 0)), PLATE_S, PLATE_S, PLATE_R)
        .extrude(-PLATE_T)
    )
    c = PLATE_S / 2 - PLATE_HOLE_INSET
    pts = [(sx * c, sz * c) for sx in (-1, 1) for sz in (-1, 1)]
    nuts = (
        cq.Workplane("XZ", origin=(0, Y_FRONT + PLATE_T, 0))
        .pushPoints(pts)
        .polygon(6, NUT_D)
        .extrude(-NUT_L)
    )
    holes = (
        cq.Workplane("XZ", origin=(0, Y_FRONT - 1.0, 0))
        .pushPoints(pts)
        .circle(PLATE_HOLE_D / 2)
        .extrude(-(PLATE_T + NUT_L + 2.0))
    )
    return p.union(nuts).cut(holes)


def tie_rod(x0, x1, y):
    rod = cq.Workplane("YZ", origin=(x0, y, 0)).circle(ROD_D / 2).extrude(x1 - x0)
    flat = cq.Workplane("XY").box(x1 - x0 + 2.0, ROD_D + 2.0, ROD_D).translate(
        ((x0 + x1) / 2, y, ROD_D / 2 - ROD_FLAT + ROD_D / 2))
    return rod.cut(flat)


result = None
for bx in beam_xs:
    b = beam_tube(beam_len).translate((bx, beam_y0, 0))
    b = b.union(foot_plate().translate((bx, 0, 0)))
    b = b.union(end_cap().translate((bx, 0, 0)))
    result = b if result is None else result.union(b)

# tie rods: run through all beams and are clamped by round nuts inside the
# two outer tubes (the nuts sit just behind the access slots)
x_in_a = beam_xs[0] - (BEAM_W / 2 - BEAM_WALL - ROD_NUT_GAP)
x_in_b = beam_xs[-1] + (BEAM_W / 2 - BEAM_WALL - ROD_NUT_GAP)
for ry in ROD_Y:
    rod = tie_rod(x_in_a + ROD_NUT_L, x_in_b - ROD_NUT_L, ry)
    for x0, dx in ((x_in_a, ROD_NUT_L), (x_in_b - ROD_NUT_L, ROD_NUT_L)):
        nut = (
            cq.Workplane("YZ", origin=(x0, ry, 0))
            .circle(ROD_NUT_D / 2)
            .extrude(dx)
        )
        rod = rod.union(nut)
    result = result.union(rod)

# access slots through the outer wall of the +X end beam
x_face = beam_xs[-1] + BEAM_W / 2
for ry in ROD_Y:
    slot = (
        rsq(cq.Workplane("YZ", origin=(x_face + 1.0, ry, 0)), SLOT_L, SLOT_H, SLOT_R)
        .extrude(-(BEAM_WALL + 2.0))
    )
    result = result.cut(slot)

VIEW = {"azimuth": 45, "elevation": 26}
